import cadquery as cq

# ======================================================================
#  Dovetail-rail mounting block with front latch (snap tongue + catch)
#  X = width, Y = depth (front face at -Y), Z = up.  Units: mm
# ======================================================================

# ---------------- driving dimensions ----------------
W = 80.0          # overall width (X)
D = 59.5          # depth of base / body (Y)
H = 31.5          # overall height
T = 2.9           # vertical edge height of the base before the flank starts

# trapezoid body / dovetail-rail profile (half widths, heights)
X_V, Z_V = 18.4, 21.4       # bottom of rail undercut (flank top)
X_TIP, Z_TIP = 24.45, 27.7  # rail edge tip
X_TOP = 20.7                # half width of the flat top

R_FLANK = 1.2     # blend between flank and base side face
R_SMALL = 0.5     # small blends on rail edges
CH_END = 0.7      # chamfer around front/back faces
CH_BOT = 0.5      # chamfer around the bottom face

# front lugs
LUG_PROJ = 10.2   # projection in front of body
LUG_H = 12.4      # height measured down from the top
LUG_CH = 2.0      # chamfer of lug top/bottom front edges
LUG_CH_V = 0.6    # chamfer of lug vertical front edges
LUG_CH_T = 0.6    # chamfer of lug top side edges
LUG_BACK = 4.7    # lug back face behind the front face
R_LUG = 1.2       # blend between left lug and front face
LUG_L = (-17.4, -9.8)
LUG_R = (10.9, 18.4)

# latch recess at front right
X_REC = 6.3       # inner wall of recess
Y_REC = 12.6      # rail cut back from front face
REC_SLOPE = 0.65  # recess face dY/dZ (leans back)
Z_SLOT = 24.4     # slot floor = latch tongue underside
CH_REC = 0.8      # chamfer on the flank / recess edge
CH_WALL = 0.35    # chamfer on the front edge of the recess wall

# slots (latch tongue)
SL_L = (7.0, 8.6)     # left slot floor at its back end
SL_L_FRONT = 11.0     # right edge of left slot at the front (tapered)
X_JOG = 8.6           # left slot edge right at the front face
SL_R = (14.95, 16.7)  # right slot floor
SLOT_BACK = 16.4      # Y of rounded slot-end centres
SLOT_CH = 0.85        # 45 deg chamfer along the slot rims

# latch head / catch tooth
HEAD_X0 = 10.9
GAP = 1.5
CATCH_TIP = (26.7, 27.6)
CATCH_TOP = 23.1
CATCH_BOT = 23.5
CATCH_SHIFT = 2.0

# front blind hole
HOLE_X, HOLE_Z = -3.15, 9.8
HOLE_D_MOUTH = 12.4                            # drafted bore: diameter at the face ...
HOLE_D, HOLE_DEPTH, HOLE_CH = 10.6, 14.0, 0.35 # ... and at the bottom; rim chamfer

# mounting holes through the flanks
MH_X, MH_Y = 32.1, 19.0
CB_D, CB_Z = 8.6, 4.6
CB_CH = 0.4       # rim chamfer of the counterbores
NUT_W, NUT_L, NUT_R, NUT_DEPTH = 4.4, 5.8, 0.8, 1.2   # rounded pocket under the counterbore
TH_D = 3.8
TH_CH = 0.6       # chamfer at the underside of the through holes

Y0 = -D / 2.0     # front face
Y1 = D / 2.0      # back face

# ---------------- body: one extruded profile ----------------
prof = [(-W / 2, 0.0), (W / 2, 0.0), (W / 2, T), (X_V, Z_V),
        (X_TIP, Z_TIP), (X_TOP, H), (-X_TOP, H), (-X_TIP, Z_TIP),
        (-X_V, Z_V), (-W / 2, T)]
body = cq.Workplane("XZ", origin=(0, Y1, 0)).polyline(prof).close().extrude(D)

# small chamfer around the bottom face, then around the front and back faces
body = body.faces("<Z").edges().chamfer(CH_BOT)
body = (body.faces("<Y or >Y").edges()
        .edges(cq.selectors.BoxSelector((-W, -D - 1, CH_BOT + 0.3), (W, D + 1, H + 1)))
        .chamfer(CH_END))
# blends on the long edges
body = body.edges("|Y").edges(cq.selectors.BoxSelector((-W, -D, T - 0.1), (W, D, T + 0.1))).fillet(R_FLANK)
body = body.edges("|Y").edges(cq.selectors.BoxSelector((-W, -D, Z_V - 0.1), (W, D, Z_V + 0.1))).fillet(R_SMALL)
body = body.edges("|Y").edges(cq.selectors.BoxSelector((-W, -D, H - 0.1), (W, D, H + 0.1))).fillet(R_SMALL)
part = body

# ---------------- latch recess (front right) ----------------
yr = Y0 + Y_REC
z_rt = T + Y_REC / REC_SLOPE
rec_prof = [(Y0 - 1, T - 1.0 / REC_SLOPE), (yr, z_rt), (yr, H + 1), (Y0 - 1, H + 1)]
recess = (cq.Workplane("YZ", origin=(X_REC, 0, 0)).polyline(rec_prof).close()
          .extrude(W / 2 + 2 - X_REC))
part = part.cut(recess)

# chamfer along the edge where the right flank meets the recess face
V = cq.Vector
n_f = V(Z_V - T, 0, W / 2 - X_V).normalized()          # flank outward normal
n_r = V(0, -1.0, REC_SLOPE).normalized()                 # recess outward normal
e_dir = n_f.cross(n_r).normalized()
if e_dir.z < 0:
    e_dir = -e_dir
p_bot = V(W / 2, Y0, T)
p_top = V(X_V, Y0 + REC_SLOPE * (Z_V - T), Z_V)
a_dir = e_dir.cross(n_f)
a_dir = a_dir if a_dir.y > 0 else -a_dir                 # into the flank face
b_dir = e_dir.cross(n_r)
b_dir = b_dir if b_dir.x < 0 else -b_dir                 # into the recess face
p0 = p_bot - e_dir * 3.0
ch_poly = [p0 + a_dir * CH_REC, p0 + a_dir * CH_REC + n_f * 0.5, p0 + (n_f + n_r) * 0.5,
           p0 + b_dir * CH_REC + n_r * 0.5, p0 + b_dir * CH_REC]
ch_face = cq.Face.makeFromWires(cq.Wire.makePolygon(ch_poly, close=True))
ch_prism = cq.Solid.extrudeLinear(ch_face, e_dir * ((p_top - p_bot).Length + 3.0))
part = part.cut(cq.Workplane().add(ch_prism))

# chamfer on the vertical front edge of the recess wall
wall_ch = (cq.Workplane("XY", origin=(0, 0, T))
           .polyline([(X_REC - CH_WALL, Y0), (X_REC, Y0 + CH_WALL), (X_REC + 0.5, Y0 + CH_WALL),
                      (X_REC + 0.5, Y0 - 0.5), (X_REC - CH_WALL, Y0 - 0.5)]).close()
           .extrude(Z_SLOT - T))
part = part.cut(wall_ch)

# ---------------- lugs ----------------
def lug(x0, x1, y_back):
    zb = H - LUG_H
    yf = Y0 - LUG_PROJ
    pts = [(yf, zb + LUG_CH), (yf + LUG_CH, zb), (Y0, zb),
           (y_back, zb + (y_back - Y0)), (y_back, H), (yf + LUG_CH, H),
           (yf, H - LUG_CH)]
    s = cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)
    s = s.edges("|Z").edges("<Y").chamfer(LUG_CH_V)
    s = s.faces(">Z").edges("|Y").chamfer(LUG_CH_T)
    return s

part = part.union(lug(*LUG_L, Y0 + LUG_BACK))
# blend the left lug into the front face
part = (part.edges(cq.selectors.BoxSelector((LUG_L[0] - 0.3, Y0 - 0.3, H - LUG_H + 0.5),
                                            (LUG_L[1] + 0.3, Y0 + 0.3, H - 0.5)))
        .edges("|Z").fillet(R_LUG))
part = part.union(lug(*LUG_R, Y0 + LUG_BACK))

# latch head joining the right lug to the tongue
head = (cq.Workplane("XY")
        .box(LUG_R[1] + 1.0 - HEAD_X0, yr - (Y0 + LUG_BACK), H - Z_SLOT, centered=False)
        .translate((HEAD_X0, Y0 + LUG_BACK, Z_SLOT)))
part = part.union(head)

# catch: small slanted dovetail tooth beside the head
y_c0 = Y0 + LUG_BACK
y_c1 = yr - GAP


def catch_prof(dx):
    return [(LUG_R[1] - 1.0, Z_SLOT), (CATCH_BOT - dx, Z_SLOT),
            (CATCH_TIP[0] - dx, CATCH_TIP[1]), (CATCH_TOP - dx, H), (LUG_R[1] - 1.0, H)]


catch = (cq.Workplane("XZ", origin=(0, y_c0, 0)).polyline(catch_prof(0.0)).close()
         .workplane(offset=-(y_c1 - y_c0)).polyline(catch_prof(CATCH_SHIFT)).close()
         .loft(ruled=True))
part = part.union(catch)
# blend the right lug into the catch
part = (part.edges(cq.selectors.BoxSelector((LUG_R[1] - 0.2, y_c0 - 0.2, Z_SLOT + 0.5),
                                            (LUG_R[1] + 0.2, y_c0 + 0.2, H - 0.5)))
        .edges("|Z").fillet(R_LUG * 0.6))

# small overhang of the top slab left of the latch, at the very front
ovh_blk = (cq.Workplane("XY").box(X_JOG + 0.5 - X_REC, 5.6, H - Z_SLOT, centered=False)
           .translate((X_REC, Y0, Z_SLOT)))
part = part.union(ovh_blk)

# ---------------- slots ----------------
def slot_wire(wp, xl, xr_back, xr_front, yb, yf, jog=None):
    """closed slot outline: round back end, straight left edge, (tapered) right edge"""
    r = (xr_back - xl) / 2
    w = (wp.moveTo(xl, yb).threePointArc((xl + r, yb + r), (xr_back, yb))
         .lineTo(xr_front, yf))
    if jog:
        for p in jog:
            w = w.lineTo(*p)
    else:
        w = w.lineTo(xl, yf)
    return w.close()


def slot_cut(xl, xr_back, xr_front, yb, yf, jog=None):
    zc = H - Z_SLOT + 1.0
    body_ = slot_wire(cq.Workplane("XY", origin=(0, 0, Z_SLOT)),
                      xl, xr_back, xr_front, yb, yf, jog).extrude(zc)
    rim = slot_wire(cq.Workplane("XY", origin=(0, 0, H - SLOT_CH)),
                    xl, xr_back, xr_front, yb, yf, jog).extrude(SLOT_CH + 1.0, taper=-45)
    return body_.union(rim)


# left slot: tapered (tongue gets narrower towards the back), open at the front
part = part.cut(slot_cut(SL_L[0], SL_L[1], SL_L_FRONT, SLOT_BACK, Y0 - 1,
                         jog=[(X_JOG, Y0 - 1), (X_JOG, Y0 + 2.7), (SL_L[0], Y0 + 5.6)]))
# 45 deg chamfer under the small overhang at the front of the left slot
ovh = (cq.Workplane("XZ", origin=(0, Y0 + 5.6, 0))
       .polyline([(X_REC, Z_SLOT), (X_JOG + 0.3, Z_SLOT), (X_JOG + 0.3, Z_SLOT + X_JOG + 0.3 - X_REC)])
       .close().extrude(6.6))
part = part.cut(ovh)
# right slot runs into the transverse gap in front of the rail end
part = part.cut(slot_cut(SL_R[0], SL_R[1], SL_R[1], SLOT_BACK, y_c1 + 0.5))
gap = (cq.Workplane("XY").box(X_TIP + 6 - SL_R[0], GAP + 0.01, H - Z_SLOT + 1.0, centered=False)
       .translate((SL_R[0], y_c1, Z_SLOT)))
part = part.cut(gap)

# ---------------- front blind hole (drafted bore, small rim chamfer) ----------------
bore = cq.Solid.makeCone(HOLE_D_MOUTH / 2, HOLE_D / 2, HOLE_DEPTH,
                         pnt=cq.Vector(HOLE_X, Y0, HOLE_Z), dir=cq.Vector(0, 1, 0))
rim = cq.Solid.makeCone(HOLE_D_MOUTH / 2 + HOLE_CH + 0.5, HOLE_D_MOUTH / 2 - 0.2, HOLE_CH + 0.7,
                        pnt=cq.Vector(HOLE_X, Y0 - 0.5, HOLE_Z), dir=cq.Vector(0, 1, 0))
part = part.cut(cq.Workplane().add(bore)).cut(cq.Workplane().add(rim))

# ---------------- counterbored mounting holes ----------------
for sx in (-1, 1):
    for sy in (-1, 1):
        x, y = sx * MH_X, sy * MH_Y
        cb = cq.Workplane("XY", origin=(x, y, CB_Z)).circle(CB_D / 2).extrude(H)
        nut = (cq.Workplane("XY", origin=(x, y, CB_Z - NUT_DEPTH))
               .rect(NUT_W, NUT_L).extrude(NUT_DEPTH + 0.5)
               .edges("|Z").fillet(NUT_R))
        th = cq.Workplane("XY", origin=(x, y, -1)).circle(TH_D / 2).extrude(H)
        csk = cq.Solid.makeCone(TH_D / 2 + TH_CH + 0.5, TH_D / 2 - 0.01, TH_CH + 0.5,
                                pnt=cq.Vector(x, y, -0.5), dir=cq.Vector(0, 0, 1))
        part = part.cut(cb).cut(nut).cut(th).cut(cq.Workplane().add(csk))

# small chamfer on the elliptical counterbore rims in the sloped flanks
rim_edges = [e for e in part.edges().vals()
             if e.geomType() == "ELLIPSE" and abs(abs(e.Center().x) - MH_X) < 1.0
             and abs(abs(e.Center().y) - MH_Y) < 1.0]
part = part.newObject(rim_edges).chamfer(CB_CH)

result = part
